"""Cable-guide mounting plate with a large through bore, an underside cable
channel and two hook clips.

Plate: D-shaped outline (rear semicircle concentric with the bore, straight
sides, rounded front corners), constant thickness.  A U-section (arched)
channel runs in the underside from the centre of the front edge into the bore.
Two hook tabs stand on the plate beside the bore, each an extruded hook
profile (post + forward-pointing hook) with a fillet at its base; the bore
wall trims the inner-rear corner of each post.
"""
import math

import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepAdaptor import BRepAdaptor_Curve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRepTools import BRepTools_WireExplorer
from OCP.Geom import Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.TopAbs import TopAbs_REVERSED
from OCP.gp import gp_Pnt, gp_Vec

# ---------------- driving dimensions (mm) ----------------
W = 80.0              # overall width (X)
R_OUT = W / 2.0       # radius of the rear semicircular end (centre = bore centre)
FRONT = 61.0          # bore centre -> flat front edge (-Y)
R_CORNER = 26.0       # front corner radius
T = 7.9               # plate thickness
R_HOLE = 36.7         # bore radius (concentric with rear arc)

# underside cable channel (front edge -> bore)
CH_W = 6.4            # channel width
CH_H = 7.2            # channel height from the bottom face (semicircular top)

# hook tabs (mirrored about X = 0)
TAB_X_IN = 30.0       # inner X face of a tab
TAB_X_OUT = 36.7      # outer X face of a tab
POST_Y_BACK = -20.1   # rear face of the post
POST_T = 6.45         # post thickness (Y)
HOOK_LEN = 6.4        # hook reach toward the front beyond the post
TAB_H = 12.9          # tab height above the plate top
HOOK_T = 6.4          # hook thickness (Z)
R_HOOK_TIP_TOP = 3.2  # rounding, hook tip top
R_HOOK_TIP_BOT = 2.7  # rounding, hook tip underside
R_TAB_BACK_TOP = 2.8  # rounding, top rear edge of the tab
R_HOOK_INNER = 0.6    # concave fillet under the hook
BASE_FILLET = 1.0     # fillet where the posts meet the plate

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- helpers ----------------
def rounded_polygon(wp, pts, radii):
    """Closed polygon on workplane `wp` with a fillet radius per vertex (0 = sharp)."""
    n = len(pts)
    segs = []
    for i in range(n):
        p0, p1, p2 = pts[i - 1], pts[i], pts[(i + 1) % n]
        r = radii[i]
        if r <= 0:
            segs.append((p1, None, p1))
            continue
        v1 = (p0[0] - p1[0], p0[1] - p1[1])
        v2 = (p2[0] - p1[0], p2[1] - p1[1])
        l1, l2 = math.hypot(*v1), math.hypot(*v2)
        u1 = (v1[0] / l1, v1[1] / l1)
        u2 = (v2[0] / l2, v2[1] / l2)
        ang = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
        d = r / math.tan(ang / 2.0)
        a = (p1[0] + u1[0] * d, p1[1] + u1[1] * d)
        b = (p1[0] + u2[0] * d, p1[1] + u2[1] * d)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.sin(ang / 2.0)
        c = (p1[0] + bis[0] * dc, p1[1] + bis[1] * dc)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        segs.append((a, m, b))
    w = wp.moveTo(*segs[0][2])
    cur = segs[0][2]
    for i in range(1, n + 1):
        a, m, b = segs[i % n]
        if math.hypot(a[0] - cur[0], a[1] - cur[1]) > 1e-6:
            w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, b)
        cur = b
    return w.close()


def _oriented_curve(edge):
    ad = BRepAdaptor_Curve(edge)
    f, l = ad.FirstParameter(), ad.LastParameter()
    tc = Geom_TrimmedCurve(BRep_Tool.Curve_s(edge, f, l), f, l)
    if edge.Orientation() == TopAbs_REVERSED:
        tc = tc.Reversed()
    return tc


def _tangent(curve, at_end):
    p, v = gp_Pnt(), gp_Vec()
    curve.D1(curve.LastParameter() if at_end else curve.FirstParameter(), p, v)
    return v.Normalized()


def join_tangent_edges(wire, ang_tol=1e-4):
    """Return the closed wire with every run of tangent-continuous lines/arcs
    merged into one exact (rational) B-spline edge, so a smooth outline gives
    one smooth side face instead of a strip of tangent faces."""
    exp = BRepTools_WireExplorer(wire.wrapped)
    curves = []
    while exp.More():
        curves.append(_oriented_curve(exp.Current()))
        exp.Next()
    n = len(curves)
    smooth = [
        _tangent(curves[i - 1], True).Angle(_tangent(curves[i], False)) < ang_tol
        for i in range(n)
    ]
    start = 0 if all(smooth) else next(i for i in range(n) if not smooth[i])
    chains, cur = [], []
    for k in range(n):
        i = (start + k) % n
        if cur and not smooth[i]:
            chains.append(cur)
            cur = []
        cur.append(curves[i])
    chains.append(cur)
    edges = []
    for ch in chains:
        if len(ch) == 1:
            edges.append(cq.Edge(BRepBuilderAPI_MakeEdge(ch[0]).Edge()))
            continue
        conv = GeomConvert_CompCurveToBSplineCurve(ch[0])
        for c in ch[1:]:
            if not conv.Add(c, 1e-6, True):
                raise RuntimeError("could not join profile edges")
        edges.append(cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge()))
    return cq.Wire.assembleEdges(edges)


def prism(profile, vec):
    """Extrude a closed profile (Workplane ending in close()) along vector `vec`."""
    wire = join_tangent_edges(profile.val())
    solid = cq.Solid.extrudeLinear(cq.Face.makeFromWires(wire), cq.Vector(*vec))
    return cq.Workplane("XY").add(solid)


# ---------------- base plate ----------------
c45 = math.cos(math.radians(45.0))
outline = (
    cq.Workplane("XY")
    .moveTo(-R_OUT, 0)
    .threePointArc((0, R_OUT), (R_OUT, 0))                       # rear semicircle
    .lineTo(R_OUT, -FRONT + R_CORNER)                            # right side
    .threePointArc(
        (R_OUT - R_CORNER + R_CORNER * c45, -FRONT + R_CORNER - R_CORNER * c45),
        (R_OUT - R_CORNER, -FRONT),
    )                                                            # front-right corner
    .lineTo(-R_OUT + R_CORNER, -FRONT)                           # front edge
    .threePointArc(
        (-R_OUT + R_CORNER - R_CORNER * c45, -FRONT + R_CORNER - R_CORNER * c45),
        (-R_OUT, -FRONT + R_CORNER),
    )                                                            # front-left corner
    .close()                                                     # left side
)
plate = prism(outline, (0, 0, T))

# central through bore (circle seam placed at the front, inside the channel)
bore = (
    cq.Workplane("XY")
    .transformed(offset=(0, 0, -1.0), rotate=(0, 0, -90))
    .circle(R_HOLE)
    .extrude(T + TAB_H + 2.0)
)
plate = plate.cut(bore)

# underside channel: U-section with semicircular top, front edge -> bore
ch_r = CH_W / 2.0
ch_len = FRONT - R_HOLE + 6.0
ch_profile = (
    cq.Workplane("XZ", origin=(0, -FRONT - 1.0, 0))
    .moveTo(-ch_r, -1.0)
    .lineTo(-ch_r, CH_H - ch_r)
    .threePointArc((0, CH_H), (ch_r, CH_H - ch_r))
    .lineTo(ch_r, -1.0)
    .close()
)
plate = plate.cut(prism(ch_profile, (0, ch_len + 1.0, 0)))


# ---------------- hook tabs ----------------
def make_tab(x_in, x_out):
    """Hook profile in the YZ plane, extruded across X from x_in to x_out."""
    yb = POST_Y_BACK
    yf = POST_Y_BACK - POST_T
    yt = yf - HOOK_LEN
    z0 = T - 1.0          # sunk into the plate so the union is clean
    zt = T + TAB_H
    zh = zt - HOOK_T
    pts = [(yb, z0), (yb, zt), (yt, zt), (yt, zh), (yf, zh), (yf, z0)]
    radii = [0, R_TAB_BACK_TOP, R_HOOK_TIP_TOP, R_HOOK_TIP_BOT, R_HOOK_INNER, 0]
    prof = rounded_polygon(cq.Workplane("YZ", origin=(x_in, 0, 0)), pts, radii)
    return prism(prof, (x_out - x_in, 0, 0))


result = plate
for sgn in (1, -1):
    xa, xb = sgn * TAB_X_IN, sgn * TAB_X_OUT
    result = result.union(make_tab(min(xa, xb), max(xa, xb)))

# base fillet around each post where it meets the plate top
for sgn in (1, -1):
    xc = sgn * (TAB_X_IN + TAB_X_OUT) / 2.0
    yc = POST_Y_BACK - POST_T / 2.0
    sel = cq.selectors.BoxSelector(
        (xc - 5.0, yc - 5.0, T - 0.3), (xc + 5.0, yc + 5.0, T + 0.3)
    )
    base_edges = [e for e in result.edges(sel).vals() if e.geomType() != "CIRCLE"]
    try:
        result = result.newObject(base_edges).fillet(BASE_FILLET)
    except Exception as exc:  # keep a valid part even if the fillet fails
        print("base fillet skipped:", exc)

# the bore wall trims the inner rear corner of each post flush
result = result.cut(bore)
